import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 151.0          # frame length along X (back face at x=0, arm ends at x=L)
HW_BACK = 66.0     # half width of frame at the back
HW_FRONT = 48.0    # half width of arms at the front end
H = 103.0          # frame height (Z) at the back
HZ_FRONT = 47.0    # half height at the front end (top/bottom taper)
CH = 34.0          # 45 deg back corner chamfer
T_BACK = 18.0      # back wall thickness
IN_HW = 47.0       # half width of the rail channel
IN_CORNER_Y = 22.0 # back wall inner face half width (45 deg inner corners)
GROOVE_W = 15.0    # vertical roller groove in the inner corner walls
GROOVE_D = 4.0
EDGE_CH = 2.0      # chamfer on the outer top/bottom edges
END_CH = 2.5       # chamfer on the vertical corners at the arm ends

TOOTH_X0 = 117.5   # start of the tooth rack along x
TOOTH_TIP = 23.0   # half width at the tooth tips
TOOTH_BASE = 29.0  # half width at tooth roots (arm end inner face)
RACK_TOP = 41.0    # inner edge of the rim at the arm ends
RACK_HZ = 46.5     # flat top of the tooth rack block
N_TEETH = 5
TOOTH_GAP = 4.0
TOOTH_HZ = 46.0    # teeth span z in [-TOOTH_HZ, TOOTH_HZ]

BAND_HZ = 26.0     # half height of the middle band (corner blocks)
CORNER_Y0 = 47.6   # inner y of the corner blocks
BACK_BAND_HZ = 11.5
HINGE_T = 2.0      # hinge plate thickness on the back of the corner blocks
HINGE_HZ = 28.0

WIN_X0, WIN_X1 = 17.0, 86.0   # spring window
WIN_H = 25.0
WIN_D = 8.0
SPRING_D = 12.5
SPRING_L = 20.0

# rollers (V pairs, top and bottom)
ROLL_R = 17.5
ROLL_W = 15.0
ROLL_Z = 33.0
ROLL_A = (44.0, 26.0)   # back roller of a pair (x, |y|)
ROLL_B = (73.5, 28.0)   # front roller of a pair (mid height)
ROLL_BR = 18.5
B_BRK = (81.0, 39.0)  # B roller bracket centre (x, |y|)
B_BRK_HZ = 16.0

# tongue (attachment plate) on the +Y side
TG_Y0, TG_Y1 = 33.0, 36.0     # plate thickness range in y
TG_X1 = 210.6                  # end of rectangular part
TG_TIP = 236.6                 # tip x
TG_HZ = 31.5                   # half height of the plate
TG_TIP_HZ = 17.0               # half height at the tip
BR_Y0, BR_Y1 = 34.0, 41.5      # base bracket y range
BR_X1 = 172.0
BR_HZ0, BR_HZ1 = 44.0, 31.5
DISC_X, DISC_R = 186.0, 9.0     # indicator disc on the +Y face of the tongue
SLOT_W, SLOT_X1 = 4.0, 172.0    # keyhole slot width and end

HZ = H / 2.0

# control points of the curved (bulged) outer side faces of the arms, x -> |y|
SIDE_PTS = [(80.0, HW_BACK - 0.5), (115.0, HW_BACK - 5.0), (140.0, HW_BACK - 13.0)]
_SIDE_SPLINE = [(CH, HW_BACK)] + SIDE_PTS + [(L - END_CH, HW_FRONT + END_CH * 0.6)]

_SIDE_EDGE = cq.Edge.makeSpline([cq.Vector(x, y, 0) for (x, y) in _SIDE_SPLINE])


def surf_y(x):
    """|y| of the curved side face at a given x (evaluated on the profile spline)"""
    if x <= CH:
        return HW_BACK
    lo, hi = 0.0, 1.0
    for _ in range(60):
        mid = 0.5 * (lo + hi)
        if _SIDE_EDGE.positionAt(mid).x < x:
            lo = mid
        else:
            hi = mid
    return _SIDE_EDGE.positionAt(lo).y


def cyl(r, h, p, d):
    return cq.Workplane().add(cq.Solid.makeCylinder(r, h, cq.Vector(*p), cq.Vector(*d)))


def hex_prism(c, a, r_flat, h):
    """hexagonal prism (socket / bolt head) centred on c, axis a"""
    e1 = cq.Vector(0, 0, 1) if abs(a.z) < 0.9 else cq.Vector(1, 0, 0)
    e2 = a.cross(e1)
    rc = r_flat / math.cos(math.pi / 6.0)
    pts = [c + e1 * (rc * math.cos(k * math.pi / 3.0)) + e2 * (rc * math.sin(k * math.pi / 3.0))
           for k in range(7)]
    return cq.Workplane().add(cq.Solid.extrudeLinear(cq.Wire.makePolygon(pts), [], a * h))


def frame_profile():
    return (cq.Workplane("XY")
            .moveTo(0, -(HW_BACK - CH))
            .lineTo(0, HW_BACK - CH)
            .lineTo(CH, HW_BACK)
            .spline(_SIDE_SPLINE[1:], includeCurrent=True)
            .lineTo(L, HW_FRONT - END_CH * 0.4)
            .lineTo(L, -HW_FRONT + END_CH * 0.4)
            .lineTo(L - END_CH, -HW_FRONT - END_CH * 0.6)
            .spline([(x, -y) for (x, y) in reversed(_SIDE_SPLINE[:-1])], includeCurrent=True)
            .close())


# side silhouette (XZ) giving the slight top/bottom taper towards the arm ends
_TAPER = [(-5.0, HZ), (40.0, HZ - 0.05), (80.0, HZ - 0.4), (115.0, HZ - 1.6),
          (L, HZ_FRONT), (L + 10.0, HZ_FRONT - 1.2)]
side = (cq.Workplane("XZ")
        .moveTo(_TAPER[0][0], -_TAPER[0][1])
        .spline([(x, -z) for (x, z) in _TAPER[1:]], includeCurrent=True)
        .lineTo(_TAPER[-1][0], _TAPER[-1][1])
        .spline([(x, z) for (x, z) in reversed(_TAPER[:-1])], includeCurrent=True)
        .close()
        .extrude(-200).translate((0, -100, 0)))

frame = frame_profile().extrude(H).translate((0, 0, -HZ))
frame = frame.intersect(side)


def outer_cap_edges(wp):
    """edges bounding the top/bottom cap faces, excluding seams between cap faces"""
    caps = [f for f in wp.faces().vals() if abs(f.normalAt().z) > 0.3]
    count = {}
    for f in caps:
        for e in f.Edges():
            key = e.hashCode()
            count.setdefault(key, [e, 0])
            count[key][1] += 1
    return [e for (e, n) in count.values() if n == 1]


frame = frame.newObject(outer_cap_edges(frame)).chamfer(EDGE_CH)

# middle band corner blocks filling the back chamfers
for s in (1, -1):
    blk = (cq.Workplane("XY")
           .polyline([(HINGE_T, s * CORNER_Y0), (HINGE_T, s * HW_BACK), (CH, s * HW_BACK),
                      (CORNER_Y0 - (HW_BACK - CH), s * CORNER_Y0)]).close()
           .extrude(2 * BAND_HZ).translate((0, 0, -BAND_HZ)))
    notch = (cq.Workplane("XY").box(6.5, 9.0, 2 * BAND_HZ + 2)
             .translate((3.0, s * 56.0, 0)))
    frame = frame.union(blk).cut(notch)
    # hinge plate with rounded ends on the back of each corner block, two screws
    hp = (cq.Workplane("XY").box(HINGE_T, 15.0, 2 * HINGE_HZ)
          .edges("|X").fillet(7.0)
          .translate((HINGE_T / 2.0, s * 57.0, 0)))
    frame = frame.union(hp)
    for z in (HINGE_HZ - 7.5, -(HINGE_HZ - 7.5)):
        # flush screw heads: annular groove plus hex socket
        frame = frame.cut(cq.Workplane("YZ").center(s * 57.0, z).circle(3.6).circle(3.0)
                          .extrude(0.6).translate((-0.1, 0, 0)))
        frame = frame.cut(hex_prism(cq.Vector(-0.1, s * 57.0, z), cq.Vector(1, 0, 0), 1.3, 1.6))

# rail channel (open through the full height)
# (back wall follows the outer chamfers with constant thickness)
channel = (cq.Workplane("XY")
           .polyline([(T_BACK, -IN_CORNER_Y), (T_BACK, IN_CORNER_Y),
                      (T_BACK + IN_HW - IN_CORNER_Y, IN_HW), (L + 40.0, IN_HW),
                      (L + 40.0, -IN_HW), (T_BACK + IN_HW - IN_CORNER_Y, -IN_HW)]).close()
           .extrude(H + 10)
           .translate((0, 0, -HZ - 5))
           .edges("|Z").fillet(4.0))
frame = frame.cut(channel)

# vertical roller grooves in the inner corner walls behind the back rollers
for s in (1, -1):
    t_wall = (ROLL_A[0] - ROLL_A[1] - T_BACK + IN_CORNER_Y) / math.sqrt(2.0)
    px = ROLL_A[0] - t_wall / math.sqrt(2.0)
    py = ROLL_A[1] + t_wall / math.sqrt(2.0)
    groove = (cq.Workplane("XY").box(GROOVE_W, GROOVE_D + 2.0, H + 10.0)
              .translate((0, (GROOVE_D + 2.0) / 2.0 - 2.0, 0))
              .rotate((0, 0, 0), (0, 0, 1), 45.0)
              .translate((px, py, 0)))
    if s < 0:
        groove = groove.mirror("XZ")
    frame = frame.cut(groove)

# narrowed arm ends (tooth rack roots)
for s in (1, -1):
    nose = (cq.Workplane("XY")
            .polyline([(108.0, s * (IN_HW + 0.5)), (TOOTH_X0, s * RACK_TOP),
                       (TOOTH_X0, s * TOOTH_BASE),
                       (L, s * TOOTH_BASE), (L, s * (IN_HW + 0.5))]).close()
            .extrude(H).translate((0, 0, -HZ)))
    frame = frame.union(nose.intersect(side))
    # the tooth rack block sits slightly below the tapered rim (flat top / bottom)
    for zs in (1, -1):
        frame = frame.cut(cq.Workplane("XY").box(L - TOOTH_X0 + 2.0, RACK_TOP - TOOTH_BASE + 1.0, 10.0)
                          .translate(((L + TOOTH_X0) / 2.0 + 1.0, s * (RACK_TOP + TOOTH_BASE - 1.0) / 2.0,
                                      zs * (RACK_HZ + 5.0))))

# tooth racks on the inner faces of the arm ends
pitch = (2 * TOOTH_HZ + TOOTH_GAP) / N_TEETH
th = pitch - TOOTH_GAP
for s in (1, -1):
    for i in range(N_TEETH):
        zc = -TOOTH_HZ + th / 2.0 + i * pitch
        tooth = (cq.Workplane("XY")
                 .box(L - TOOTH_X0, TOOTH_BASE - TOOTH_TIP + 0.5, th)
                 .translate(((L + TOOTH_X0) / 2.0,
                             s * (TOOTH_TIP + TOOTH_BASE + 0.5) / 2.0, zc))
                 .edges("|X and %s and >Z" % (">Y" if s < 0 else "<Y")).chamfer(2.5))
        frame = frame.union(tooth)

# ---------------- side face features (both sides, mirror symmetric) ----------------
for s in (1, -1):
    # spring window pocket
    win = (cq.Workplane("XY").box(WIN_X1 - WIN_X0, 40.0, WIN_H)
           .translate(((WIN_X0 + WIN_X1) / 2.0, s * (HW_BACK + 20.0 - WIN_D), 0)))
    frame = frame.cut(win)
    # through holes and screw counterbores, drilled along Y
    for (x, z, d, depth) in [(55.0, 39.0, 7.0, 14.0), (55.0, -39.0, 7.0, 14.0),
                             (55.0, 25.0, 9.8, 25.0), (55.0, -25.0, 9.8, 25.0),
                             (128.0, 0.0, 10.5, 3.0), (128.0, 0.0, 5.0, 16.0),
                             (140.7, 37.5, 11.0, 4.0), (140.7, -37.5, 11.0, 4.0),
                             ]:
        y_in = surf_y(x) - depth
        y_out = HW_BACK + 5.0
        frame = frame.cut(cyl(d / 2.0, y_out - y_in, (x, s * y_out, z), (0, -s, 0)))
    # small vertical slot next to the centre hole
    frame = frame.cut(cq.Workplane("XZ").center(113.6, 0.0).slot2D(5.5, 3.0, 90.0)
                      .extrude(12.0, both=True)
                      .translate((0, s * surf_y(113.6), 0)))
    # socket screws sitting in the counterbores
    for (x, z) in [(140.7, 37.5), (140.7, -37.5)]:
        y0 = surf_y(x) - 4.0
        head = cyl(4.2, 3.0, (x, s * y0, z), (0, s, 0))
        hexs = hex_prism(cq.Vector(x, s * (y0 + 1.0), z), cq.Vector(0, s, 0), 1.6, 3.0)
        frame = frame.union(head).cut(hexs)
    # oval holes on the back chamfer faces (top and bottom bands)
    for z in (34.0, -34.0):
        d = cq.Vector(-1.0, s * 1.0, 0).normalized()
        c = cq.Vector(18.0, s * (HW_BACK - CH + 18.0), z)
        hole = cq.Solid.makeCylinder(3.5, 30.0, c - d * 15.0, d)
        frame = frame.cut(cq.Workplane().add(hole))
        # hex bolt head with washer, sitting in a counterbore
        frame = frame.cut(cq.Workplane().add(cq.Solid.makeCylinder(6.8, 10.0, c - d * 4.5, d)))
        c = c - d * 4.5
        washer = cq.Workplane().add(cq.Solid.makeCylinder(5.5, 1.0, c, d))
        frame = frame.union(washer).union(hex_prism(c + d * 1.0, d, 4.3, 3.5))

# thin raised band across the back face
frame = frame.union(cq.Workplane("XY").box(1.0, 2 * (HW_BACK - CH) - 1.0, 2 * BACK_BAND_HZ)
                    .translate((-0.5, 0, 0)))

# back face holes
for (y, z, d) in [(0.0, 37.0, 4.5), (12.0, 30.0, 3.0), (0.0, -37.0, 4.5)]:
    frame = frame.cut(cyl(d / 2.0, 12.0, (-1.0, y, z), (1, 0, 0)))

# spring in each window (plain cylinder with coil grooves)
for s in (1, -1):
    yc = s * (HW_BACK - WIN_D + 0.5)
    frame = frame.union(cyl(SPRING_D / 2.0, SPRING_L, (WIN_X0, yc, 0), (1, 0, 0)))
    for k in range(5):
        g = cq.Solid.makeTorus(SPRING_D / 2.0 + 0.2, 0.8,
                               cq.Vector(WIN_X0 + 2.5 + k * 3.6, yc, 0), cq.Vector(1, 0, 0))
        frame = frame.cut(cq.Workplane().add(g))

# ---------------- rollers inside the channel ----------------
r2 = 1.0 / math.sqrt(2.0)


def roller(c, a, r, w):
    body = cq.Workplane().add(cq.Solid.makeCylinder(r, w, c - a * (w / 2.0), a)).edges().fillet(2.0)
    face = c + a * (w / 2.0)
    hub = cyl(r * 0.5, 1.0, tuple(face - a * 0.5), tuple(a))
    ring = cq.Solid.makeTorus(r * 0.72, 0.6, face, a)
    head = cyl(r * 0.3, 2.5, tuple(face), tuple(a))
    sock = hex_prism(face + a * 1.0, a, r * 0.13, 2.0)
    return body.union(hub).cut(cq.Workplane().add(ring)).union(head).cut(sock)


for s in (1, -1):
    # back rollers (top and bottom), axles into the back corners
    for zs in (1, -1):
        c = cq.Vector(ROLL_A[0], s * ROLL_A[1], zs * ROLL_Z)
        a = cq.Vector(r2, -s * r2, 0.0)
        frame = frame.union(roller(c, a, ROLL_R, ROLL_W))
        frame = frame.union(cyl(5.0, 30.0, tuple(c), (-r2, s * r2, 0.0)))
        # bearing boss on the inner chamfer wall
        frame = frame.union(cyl(9.0, 13.0, tuple(c - a * (ROLL_W / 2.0 - 0.5)), (-r2, s * r2, 0.0)))
    # front roller at mid height, axle into a bracket on the arm wall
    c = cq.Vector(ROLL_B[0], s * ROLL_B[1], 0.0)
    a = cq.Vector(r2, s * r2, 0.0)
    frame = frame.union(roller(c, a, ROLL_BR, ROLL_W))
    frame = frame.union(cyl(5.0, 30.0, tuple(c), (r2, s * r2, 0.0)))
    brk = (cq.Workplane("XY").box(14.0, 26.0, 2 * B_BRK_HZ)
           .rotate((0, 0, 0), (0, 0, 1), s * 45.0)
           .translate((B_BRK[0], s * B_BRK[1], 0.0)))
    brk = brk.intersect(cq.Workplane("XY").box(60.0, 30.0, 2 * B_BRK_HZ)
                        .translate((B_BRK[0], s * (IN_HW + 0.5 - 15.0), 0.0)))
    frame = frame.union(brk)
    for zs in (1, -1):
        # countersunk screw recess in the bracket top / bottom
        frame = frame.cut(cq.Workplane().add(cq.Solid.makeCone(
            1.2, 3.2, 2.0, cq.Vector(83.4, s * 39.5, zs * (B_BRK_HZ - 2.0)), cq.Vector(0, 0, zs))))
        # cone pins on the back wall
        frame = frame.union(cq.Workplane().add(
            cq.Solid.makeCone(3.0, 1.2, 8.0, cq.Vector(T_BACK - 0.5, s * 12.5, zs * 35.0),
                              cq.Vector(1, 0, 0))))

# rib across the inner back wall at mid height
frame = frame.union(cq.Workplane("XY").box(3.5, 2 * IN_CORNER_Y, 25.0)
                    .translate((T_BACK + 1.25, 0, 0)))

# through holes in the back wall
for z in (25.0, -25.0):
    frame = frame.cut(cyl(4.3, T_BACK + 2.0, (-1.0, 0.0, z), (1, 0, 0)))

# ---------------- tongue / attachment plate ----------------
bracket = (cq.Workplane("XZ")
           .polyline([(L - 2.0, -BR_HZ0), (L - 2.0, BR_HZ0), (BR_X1, BR_HZ1),
                      (BR_X1, -BR_HZ1)]).close()
           .extrude(-(BR_Y1 - BR_Y0)).translate((0, BR_Y0, 0)))
plate = (cq.Workplane("XZ")
         .polyline([(L - 1.0, -TG_HZ), (L - 1.0, TG_HZ), (TG_X1, TG_HZ),
                    (TG_TIP, TG_TIP_HZ), (TG_TIP, -TG_TIP_HZ), (TG_X1, -TG_HZ)]).close()
         .extrude(-(TG_Y1 - TG_Y0)).translate((0, TG_Y0, 0)))
tongue = bracket.union(plate)
# base pad on the -Y face with the keyhole slot and two button heads
pad = (cq.Workplane("XZ").center((L + 178.0) / 2.0, 0).rect(178.0 - L, 2 * TG_HZ)
       .extrude(1.5).translate((0, TG_Y0, 0)).edges("|Y").fillet(3.0))
tongue = tongue.union(pad)
# keyhole slot with a funnel entry, open towards the frame
slot = (cq.Workplane("XZ")
        .moveTo(L - 3.0, SLOT_W / 2.0 + 4.0)
        .lineTo(L + 1.5, SLOT_W / 2.0 + 4.0)
        .lineTo(L + 6.5, SLOT_W / 2.0)
        .lineTo(SLOT_X1 - SLOT_W / 2.0, SLOT_W / 2.0)
        .threePointArc((SLOT_X1, 0.0), (SLOT_X1 - SLOT_W / 2.0, -SLOT_W / 2.0))
        .lineTo(L + 6.5, -SLOT_W / 2.0)
        .lineTo(L + 1.5, -SLOT_W / 2.0 - 4.0)
        .lineTo(L - 3.0, -SLOT_W / 2.0 - 4.0)
        .close()
        .extrude(-(TG_Y1 - TG_Y0 + 4.0)).translate((0, TG_Y0 - 2.0, 0)))
tongue = tongue.cut(slot)
for z in (17.0, -17.0):
    head = (cq.Workplane("XZ").center(159.6, z).circle(4.0).extrude(2.5)
            .translate((0, TG_Y0 - 1.5, 0)).faces("<Y").edges().fillet(1.5))
    tongue = tongue.union(head)
    tongue = tongue.cut(hex_prism(cq.Vector(159.6, TG_Y0 - 4.1, z), cq.Vector(0, 1, 0), 1.3, 1.8))
# indicator disc (ring groove with a pointer slot) on the +Y face of the plate
disc_groove = (cq.Workplane("XZ").center(DISC_X, 0).circle(DISC_R).circle(DISC_R - 1.0)
               .extrude(-1.0).translate((0, TG_Y1 - 0.6, 0)))
tongue = tongue.cut(disc_groove)
pointer = (cq.Workplane("XZ").center(DISC_X - 2.0, -1.0).slot2D(10.0, 1.6)
           .extrude(-1.0).translate((0, TG_Y1 - 0.6, 0)))
tongue = tongue.cut(pointer)
# shallow rib pockets and the tip tray
for (z0, z1) in [(21.0, 28.7), (3.7, 11.4), (-13.6, -5.9), (-30.0, -22.3)]:
    pk = (cq.Workplane("XY").box(210.0 - 178.0, 2.0, z1 - z0)
          .translate(((178.0 + 210.0) / 2.0, TG_Y0, (z0 + z1) / 2.0)))
    tongue = tongue.cut(pk)
tray = (cq.Workplane("XY").box(TG_TIP - 1.5 - TG_X1, 3.0, 33.0)
        .translate(((TG_X1 + TG_TIP - 1.5) / 2.0, TG_Y0, -0.6)))
tongue = tongue.cut(tray)

result = frame.union(tongue)
